import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
W = 48.0          # overall width (X)
H = 70.0          # overall height (Z)
COL_H = 14.6      # height of the top column above the upper arm
T_ARM = 8.9       # upper arm thickness
SLOT_H = 22.95    # clamp slot height
T_LOW = 8.95      # thickness of the rear C-frame lower arm
T_WALL = 10.4     # thickness of the vertical back wall (+X side)
COL_W = 24.0      # width of the top column (X)
D_FRONT = 19.5    # depth of the front block (Y)
D_BACK = 13.3     # depth of the rear C-frame band (Y)
R_CORNER = 8.2    # outer corner radius of the rear C-frame

HOLE_X = 8.4      # clamp hole distance from the open (-X) end
HOLE_D_TOP = 9.0  # clearance hole through the upper arm
HOLE_D_LOW = 7.8  # hole through the lower block
SIDE_HOLE_D = 9.0 # side hole diameter (through back wall)

NUT_AF = 14.5     # hex nut pocket across flats (inside face of back wall)
NUT_DEPTH = 6.0   # hex nut pocket depth

RING_D = 14.5     # raised ring base diameter around the clamp holes
RING_H = 1.1      # raised ring height
LOW_CSK_D = 8.8   # enlarged upper part of the lower hole
LOW_CSK_DEPTH = 8.0  # its depth from the ring top

# ---------------- derived levels ----------------
Z_ARM_TOP = H - COL_H
Z_ARM_BOT = Z_ARM_TOP - T_ARM
Z_LOW_TOP = Z_ARM_BOT - SLOT_H
Z_FRAME_BOT = Z_LOW_TOP - T_LOW
D = D_FRONT + D_BACK
X_WALL = W - T_WALL
HOLE_Y = D_FRONT / 2.0
Z_SIDE = (Z_ARM_BOT + Z_LOW_TOP) / 2.0

# ---------------- C-frame through the full depth ----------------
frame_outer = (
    cq.Workplane("XY")
    .box(W, D, Z_ARM_TOP - Z_FRAME_BOT, centered=False)
    .translate((0, 0, Z_FRAME_BOT))
)
frame_outer = frame_outer.edges("|Y and >X").fillet(R_CORNER)
slot = (
    cq.Workplane("XY")
    .box(X_WALL + 1.0, D + 2.0, SLOT_H, centered=False)
    .translate((-1.0, -1.0, Z_LOW_TOP))
)
frame = frame_outer.cut(slot)

# ---------------- front block: top column + lower block ----------------
column = (
    cq.Workplane("XY")
    .box(COL_W, D_FRONT, H - Z_ARM_BOT, centered=False)
    .translate((W - COL_W, 0, Z_ARM_BOT))
)
lower = cq.Workplane("XY").box(W, D_FRONT, Z_LOW_TOP, centered=False)

body = frame.union(column).union(lower)


# ---------------- raised rings around the clamp holes ----------------
def ring_up(r_in, seam_deg=135.0):
    """Low rounded ring (revolved profile) standing on z=0, pointing +Z.
    Rounded (convex) flank rising from the base to the hole edge."""
    rb = RING_D / 2.0
    prof = (
        cq.Workplane("XZ")
        .moveTo(r_in, 0)
        .lineTo(rb, 0)
        .spline([(r_in, RING_H)], tangents=[(0, 1), (-1, 0)],
                includeCurrent=True)
        .close()
        .revolve(360, (0, 0, 0), (0, 1, 0))
    )
    # turn the revolve seam to the side facing away from the usual views
    return prof.rotate((0, 0, 0), (0, 0, 1), seam_deg)


ring_low = ring_up(LOW_CSK_D / 2.0 - 0.05).translate((HOLE_X, HOLE_Y, Z_LOW_TOP))
ring_top = (
    ring_up(HOLE_D_TOP / 2.0 - 0.05, seam_deg=225.0)
    .rotate((0, 0, 0), (1, 0, 0), 180)
    .translate((HOLE_X, HOLE_Y, Z_ARM_BOT))
)
body = body.union(ring_low).union(ring_top)

# ---------------- clamp holes ----------------
def zcyl(d, z0, length, seam_deg=-45.0):
    """Vertical cylinder at the clamp hole axis, seam turned away from view."""
    c = (
        cq.Workplane("XY")
        .circle(d / 2.0)
        .extrude(length)
        .rotate((0, 0, 0), (0, 0, 1), seam_deg)
    )
    return c.translate((HOLE_X, HOLE_Y, z0))


hole_top = zcyl(HOLE_D_TOP, Z_ARM_BOT - 2.0, H - Z_ARM_BOT + 4.0)
hole_low = zcyl(HOLE_D_LOW, -2.0, Z_LOW_TOP + 4.0)
# the upper part of the lower hole is slightly larger (step well inside)
csk = zcyl(LOW_CSK_D, Z_LOW_TOP + RING_H - LOW_CSK_DEPTH, LOW_CSK_DEPTH + 2.0)
body = body.cut(hole_top).cut(hole_low).cut(csk)

# ---------------- side hole + hex nut pocket in the back wall ----------------
shole = (
    cq.Workplane("YZ")
    .circle(SIDE_HOLE_D / 2.0)
    .extrude(T_WALL + 2.0)
    .rotate((0, 0, 0), (1, 0, 0), 180)   # seam to the front (-Y) side
    .translate((X_WALL - 1.0, HOLE_Y, Z_SIDE))
)
r_hex = NUT_AF / math.sqrt(3.0)
hex_pts = [
    (HOLE_Y + r_hex * math.cos(math.radians(30 + 60 * i)),
     Z_SIDE + r_hex * math.sin(math.radians(30 + 60 * i)))
    for i in range(6)
]
nut = (
    cq.Workplane("YZ")
    .polyline(hex_pts)
    .close()
    .extrude(NUT_DEPTH + 1.0)
    .translate((X_WALL - 1.0, 0, 0))
)
body = body.cut(shole).cut(nut)

result = body.clean()

VIEW = {"azimuth": 45, "elevation": 26}
